import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# mounting plate (X along length, Y across, top face at Z=0)
PLATE_L = 100.0
PLATE_W = 80.0
PLATE_T = 5.3

# stand-off bosses on top of the plate
BOSS_D = 15.5
BOSS_H = 9.9
BOSS_HOLE_D = 8.5
BOSS_X = (10.0, 46.5)          # from the left plate edge
BOSS_Y = 30.0                  # +/- from plate centre line

# rectangular window through the plate
SLOT_CX = 78.4
SLOT_LX = 20.2
SLOT_LY = 36.5
SLOT_R = 0.0                   # corner radius in plan (0 = sharp)
SLOT_EDGE_R = 2.0              # rounded lower edge of the window

# curved arm (profile in XZ, extruded across Y)
ARM_W = 17.5                   # width across Y
ARM_FILLET = 3.0               # blend into the plate underside
# outer edge: quarter ellipse whose lowest point is the ring bottom
ARM_OUT_CX = 112.9
ARM_OUT_A = 98.85
ARM_OUT_B = 173.8
# inner edge: quarter ellipse whose lowest point sits on the ring top at
# the bore edge (centre X derived below)
ARM_IN_A = 73.7
ARM_IN_B = 137.1

# pipe clamp ring (vertical axis)
RING_CX = 136.5
RING_OD = 54.0
RING_ID = 40.2
RING_H = 25.4
RING_ZB = -170.9               # bottom of ring

# split clamp ears
EAR_T = 5.8                    # thickness of each ear
EAR_GAP = 6.6                  # clamping slot width
EAR_END_X = 176.3              # tip of the ears
EAR_R = 7.0                    # tip corner rounding
EAR_HOLE_D = 9.0
EAR_HOLE_X = 168.6

# ---------------- derived ----------------
ring_zt = RING_ZB + RING_H
ring_zc = RING_ZB + RING_H / 2.0
ring_r = RING_OD / 2.0
ring_left = RING_CX - ring_r
ARM_IN_CX = RING_CX - RING_ID / 2.0

# ---------------- plate ----------------
plate = (
    cq.Workplane("XY")
    .box(PLATE_L, PLATE_W, PLATE_T, centered=(False, True, False))
    .translate((0, 0, -PLATE_T))
)

# bosses
boss_pts = [(x, s * BOSS_Y) for x in BOSS_X for s in (-1, 1)]


def zcyl(x, y, r, z0, h, seam_deg):
    """Vertical cylinder with its parametric seam turned to seam_deg."""
    c = cq.Solid.makeCylinder(r, h, cq.Vector(0, 0, z0), cq.Vector(0, 0, 1))
    c = c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam_deg)
    return c.translate(cq.Vector(x, y, 0))


for (bx, by) in boss_pts:
    plate = plate.union(zcyl(bx, by, BOSS_D / 2.0, 0.0, BOSS_H, 135.0))

# ---------------- arm ----------------
# The arm is the band between two quarter ellipses (outer / inner edge
# as seen from the front), clipped to the space between plate and ring.
z_top = -PLATE_T / 2.0         # arm runs up into the plate
z_pl = -PLATE_T                # plate underside


def ell_prism(cx, cz, a, b, depth):
    """Elliptic cylinder along Y, centred at (cx, cz) in the XZ plane."""
    return (
        cq.Workplane("XZ")
        .workplane(offset=-depth / 2.0)      # XZ normal is -Y
        .center(cx, cz)
        .ellipse(a, b)
        .extrude(depth)
    )


arm_clip = (
    cq.Workplane("XY")
    .box(ARM_IN_CX, ARM_W, z_top - RING_ZB, centered=(False, True, False))
    .translate((0, 0, RING_ZB))
)
outer_ell = ell_prism(ARM_OUT_CX, RING_ZB + ARM_OUT_B, ARM_OUT_A, ARM_OUT_B, ARM_W + 2)
inner_ell = ell_prism(ARM_IN_CX, ring_zt + ARM_IN_B, ARM_IN_A, ARM_IN_B, ARM_W + 4)
arm = arm_clip.intersect(outer_ell).cut(inner_ell)

body = plate.union(arm)

# fillet the arm-to-plate junction (edges lying in the plate underside)
try:
    body = body.edges(
        cq.selectors.BoxSelector(
            (1.0, -ARM_W / 2 - 1, z_pl - 0.5),
            (PLATE_L - 1.0, ARM_W / 2 + 1, z_pl + 0.5),
        )
    ).fillet(ARM_FILLET)
except Exception:
    pass

# ---------------- ring + ears ----------------
ring = (
    cq.Workplane("XY")
    .workplane(offset=RING_ZB)
    .center(RING_CX, 0)
    .circle(ring_r)
    .extrude(RING_H)
)

ear_w = EAR_GAP + 2 * EAR_T
ears = (
    cq.Workplane("XY")
    .box(EAR_END_X - RING_CX, ear_w, RING_H, centered=(False, True, False))
    .translate((RING_CX, 0, RING_ZB))
    .edges("|Y and >X")
    .fillet(EAR_R)
)
clamp = ring.union(ears)

body = body.union(clamp)

# bore
bore = (
    cq.Workplane("XY")
    .workplane(offset=RING_ZB - 1)
    .center(RING_CX, 0)
    .circle(RING_ID / 2.0)
    .extrude(RING_H + 2)
)
body = body.cut(bore)

# clamping slot through the wall and between the ears
gap = (
    cq.Workplane("XY")
    .box(EAR_END_X - RING_CX + 5, EAR_GAP, RING_H + 2, centered=(False, True, False))
    .translate((RING_CX, 0, RING_ZB - 1))
)
body = body.cut(gap)

# bolt hole through the ears (along Y)
bolt = (
    cq.Workplane("XZ")
    .workplane(offset=-ear_w)
    .center(EAR_HOLE_X, ring_zc)
    .circle(EAR_HOLE_D / 2.0)
    .extrude(2 * ear_w)
)
body = body.cut(bolt)

# ---------------- plate holes and window ----------------
for (bx, by) in boss_pts:
    body = body.cut(
        zcyl(bx, by, BOSS_HOLE_D / 2.0, -PLATE_T - 1, PLATE_T + BOSS_H + 2, -45.0)
    )

window = (
    cq.Workplane("XY")
    .workplane(offset=-PLATE_T - 1)
    .center(SLOT_CX, 0)
    .rect(SLOT_LX, SLOT_LY)
    .extrude(PLATE_T + 2)
)
if SLOT_R > 0:
    window = window.edges("|Z").fillet(SLOT_R)
body = body.cut(window)

# round over the lower edge of the window
try:
    body = body.edges(
        cq.selectors.BoxSelector(
            (SLOT_CX - SLOT_LX / 2 - 1, -SLOT_LY / 2 - 1, -PLATE_T - 0.1),
            (SLOT_CX + SLOT_LX / 2 + 1, SLOT_LY / 2 + 1, -PLATE_T + 0.1),
        )
    ).fillet(SLOT_EDGE_R)
except Exception:
    pass

result = body.clean()

VIEW = {"azimuth": 45, "elevation": 26}
